import math
import cadquery as cq

# =====================================================================
#  Safety laser scanner housing: D-shaped body (flat rear, round front),
#  conical optics window with a cap on top, M12 connectors underneath.
# =====================================================================

# ---------------- housing ----------------
R_BODY = 36.5        # radius of the round (front/right) part of the lower housing
X_BACK = -39.25      # flat rear face (-X) of the lower housing
Z_BAND = 53.7        # step between lower housing and the (slightly smaller) top band
BAND_INSET = 0.8     # the top band is inset by this much
H_BODY = 69.0        # housing height (at the ring)
TOP_SLOPE = 0.24     # the housing top falls away from the ring as a shallow cone
R_TOP_EDGE = 1.2     # rounding of the housing top edge
R_BOT_EDGE = 0.8     # rounding of the housing bottom edge

GROOVE_W = 0.6       # width of parting seams
GROOVE_D = 0.35      # depth of parting seams

# inclined parting seam of the lower cover (in XZ, symmetric in Y)
SEAM_Z_BACK = 23.0   # seam height at the rear face
SEAM_X_KNEE = 21.25  # seam becomes horizontal here
SEAM_Z_LOW = 6.4     # height of horizontal seam part

# ---------------- optics head (revolved) ----------------
R_RING = 35.3        # mounting ring radius
Z_RING_WALL = 72.6   # top of ring cylindrical wall
R_RING_IN = 25.6
Z_RING_TOP = 75.4
R_CONE_BOT = 24.7
Z_CONE_BOT = 76.2
R_CONE_TOP = 32.35
Z_CONE_TOP = 93.25
R_CONE_LIP = 32.6
Z_CAP_BOT = 96.4
R_CAP_BOT = 34.2
R_CAP_TOP = 32.8
Z_CAP_EDGE = 109.2
CAP_EDGE_FILLET = 1.1
R_STEP = 20.7
STEP_FILLET = 1.3
R_PLATEAU = 19.3
Z_PLATEAU = 111.2
HEAD_SEAM_ANGLE = 90.0   # where the revolve seam sits (hidden at the back)

# ---------------- screw bosses ----------------
BOSS_W = 7.5
BOSS_H = 7.2
BOSS_PROUD = 1.4                # outer face distance from the lower housing wall (side faces)
BOSS_PROUD_BACK = 0.9           # same, rear face
BOSS_Z = 57.9
BOSS_X_SIDE = (-32.0, 3.5)      # on -Y and +Y faces
BOSS_Y_BACK = (-26.0, 26.0)     # on -X face

# ---------------- connectors ----------------
CONN_X = -26.6
CONN_Y = (-22.8, -7.6, 7.6, 22.8)
CONN_BASE_R = 4.9    # flange at the housing
CONN_BASE_H = 2.7
CONN_NUT_AF = 7.6    # hex neck
CONN_NECK_H = 3.0
CONN_TIP_R = 4.3     # coupling end
CONN_LEN = 7.4

# ---------------- rear connector pocket ----------------
POCKET_W = 59.0
POCKET_H = 19.5
POCKET_D = 3.5
POCKET2_W = 55.0
POCKET2_H = 3.5
POCKET2_D = 6.0

# ---------------- side window (+X) ----------------
WIN_HALF_W = 13.0
WIN_Z_TOP = 51.6
WIN_Z_SIDE = 32.0
WIN_Z_LOW = 29.0
WIN_X_FLOOR_TOP = 33.9    # recess floor is tilted: shallow at the top
WIN_X_FLOOR_BOT = 32.8    # ... deeper at the bottom
WIN_CREASE = ((-4.1, 50.75), (-10.6, 32.6))   # (y, z) ends of the floor crease
WIN_FACET_DROP = 1.3      # extra depth of the floor facet at the -Y wall

# ---------------- misc ----------------
PLUG_Z = 61.9        # slotted plug in the top band (+X)
PLUG_R = 4.1
PLUG_PROUD = 1.9
LABEL = (-33.5, -11.7, 20.5, 49.5)   # x0, x1, z0, z1 of laser label frame on +Y face
PANEL_X1 = -7.0                      # right edge of the shallow panel on the -Y face
CORNER_NOTCH_X = (X_BACK, -33.1)     # screw notches at the rear top corners (x extent)
CORNER_NOTCH_Y = (-34.6, -30.5)      # (y extent, mirrored for +Y)
CORNER_NOTCH_Z = 64.2                # notch floor
CORNER_SCREW = (-35.85, 32.55)
LOGO_H = 11.5
LOGO_X = 3.6
LOGO_Z = 33.0


def d_outline(o=0.0, z0=0.0):
    """Closed D-shaped outline (flat rear, round front) of the housing, offset outward by o."""
    r = R_BODY + o
    xb = X_BACK - o
    return (cq.Workplane("XY").workplane(offset=z0)
            .moveTo(0, -r)
            .lineTo(xb, -r)
            .lineTo(xb, r)
            .lineTo(0, r)
            .threePointArc((r, 0), (0, -r))
            .close())


def d_prism(o, z0, h):
    return d_outline(o, z0).extrude(h)


def top_limit(raise_by=0.0):
    """Solid of revolution bounding the housing from above: a shallow cone falling away from the ring."""
    r_out = 70.0
    z_out = H_BODY + raise_by - TOP_SLOPE * (r_out - R_RING)
    z_in = H_BODY + raise_by + TOP_SLOPE * R_RING
    return (cq.Workplane("XZ")
            .polyline([(0, -5), (r_out, -5), (r_out, z_out), (0, z_in)])
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))


def housing(o=0.0):
    lower = d_prism(o, 0.0, Z_BAND)
    band = d_prism(o - BAND_INSET, Z_BAND - 0.5, H_BODY - Z_BAND + 20.0)
    return lower.union(band).intersect(top_limit(o))


def skin(depth):
    """Thin shell region just under the outer surface of the lower housing."""
    return d_prism(4.0, -1.0, H_BODY + 2).cut(d_prism(-depth, -2.0, H_BODY + 4))


# ------------------------------------------------------------------ housing
body = housing(0.0)
top_edges = [e for e in body.edges().vals()
             if e.BoundingBox().zmin > Z_BAND + 5.0 and e.geomType() != "LINE"]
body = body.newObject(top_edges).fillet(R_TOP_EDGE)
body = body.faces("<Z").edges().fillet(R_BOT_EDGE)

# inclined seam of the lower cover
hw = GROOVE_W / 2
x_a, x_b = X_BACK - 5.0, R_BODY + 5.0
slope = (SEAM_Z_LOW - SEAM_Z_BACK) / (SEAM_X_KNEE - X_BACK)
za = SEAM_Z_BACK + slope * (x_a - X_BACK)


def seam_z(x):
    if x >= SEAM_X_KNEE:
        return SEAM_Z_LOW
    return SEAM_Z_BACK + slope * (x - X_BACK)


seam_band = (cq.Workplane("XZ")
             .polyline([(x_a, za + hw), (SEAM_X_KNEE, SEAM_Z_LOW + hw), (x_b, SEAM_Z_LOW + hw),
                        (x_b, SEAM_Z_LOW - hw), (SEAM_X_KNEE, SEAM_Z_LOW - hw), (x_a, za - hw)])
             .close()
             .extrude(60, both=True))
body = body.cut(skin(GROOVE_D).intersect(seam_band))

# short vertical seams of the bottom cover, below the seam knee (both sides)
for sy in (-1, 1):
    a_b = math.radians(57.0)
    vx, vy = R_BODY * math.cos(a_b), sy * R_BODY * math.sin(a_b)
    vb = (cq.Workplane("XY").box(8.0, GROOVE_W, SEAM_Z_LOW + 1.0, centered=(False, True, False))
          .rotate((0, 0, 0), (0, 0, 1), sy * 57.0)
          .translate((vx - 4.0 * math.cos(a_b), vy - sy * 4.0 * math.sin(a_b), -1.0)))
    body = body.cut(skin(GROOVE_D).intersect(vb))

# vertical seam below the side window
vseam = cq.Workplane("XY").box(10, GROOVE_W, 40, centered=(False, True, False)).translate((30.0, -WIN_HALF_W - 0.6, 0))
body = body.cut(skin(GROOVE_D).intersect(vseam).intersect(
    cq.Workplane("XY").box(200, 200, WIN_Z_SIDE - SEAM_Z_LOW, centered=(True, True, False)).translate((0, 0, SEAM_Z_LOW))))

# shallow panel on the flat front face (-Y)
panel = (cq.Workplane("XZ")
         .polyline([(X_BACK - 2, Z_BAND - 0.6), (PANEL_X1, Z_BAND - 0.6),
                    (PANEL_X1, seam_z(PANEL_X1) + 0.6), (X_BACK - 2, seam_z(X_BACK - 2) + 0.6)])
         .close()
         .extrude(-3.0)                     # XZ normal is -Y: negative extrude goes toward +Y
         .translate((0, -R_BODY - 2.7, 0)))
body = body.cut(panel)

# laser warning label on the flat back face (+Y): recessed frame with a plate
lx0, lx1, lz0, lz1 = LABEL
body = body.cut(cq.Workplane("XY").box(lx1 - lx0, 2.0, lz1 - lz0)
                .translate(((lx0 + lx1) / 2, R_BODY + 1.0 - 0.4, (lz0 + lz1) / 2)))
plate_w = 13.3
body = body.union(cq.Workplane("XY").box(plate_w, 0.5, lz1 - lz0 - 2.0)
                  .edges("|Y").fillet(0.8)
                  .translate((lx0 + 1.0 + plate_w / 2, R_BODY - 0.4 + 0.25, (lz0 + lz1) / 2)))

# rear connector pocket (open to -X and to the bottom)
for (pd, pw, ph) in ((POCKET_D, POCKET_W, POCKET_H), (POCKET2_D, POCKET2_W, POCKET2_H)):
    body = body.cut(cq.Workplane("XY").box(pd + 2, pw, ph + 2, centered=(False, True, False))
                    .translate((X_BACK - 2, 0, -2)))

# slotted sealing plug inside the pocket
px = X_BACK + POCKET_D
PP_Y, PP_Z, PP_R = -16.2, 10.2, 4.6
plug2 = (cq.Workplane("YZ").workplane(offset=px).center(PP_Y, PP_Z)
         .circle(PP_R).extrude(-1.2)
         .faces("<X").chamfer(0.4))
plug2 = plug2.cut(cq.Workplane("XY").box(1.0, 2 * PP_R + 1, 0.8).translate((px - 1.2, PP_Y, PP_Z))
                  .rotate((px, PP_Y, PP_Z), (px + 1, PP_Y, PP_Z), 60))
body = body.union(plug2)

# side window recess (+X): outline in YZ, floor tilted (deeper towards the bottom)
win = (cq.Workplane("YZ").workplane(offset=25.0)
       .moveTo(-WIN_HALF_W, WIN_Z_TOP)
       .lineTo(-WIN_HALF_W + 0.4, WIN_Z_SIDE)
       .threePointArc((0, WIN_Z_LOW), (WIN_HALF_W - 0.4, WIN_Z_SIDE))
       .lineTo(WIN_HALF_W, WIN_Z_TOP)
       .close()
       .extrude(20))
tilt = math.degrees(math.atan2(WIN_X_FLOOR_TOP - WIN_X_FLOOR_BOT, WIN_Z_TOP - WIN_Z_LOW))
floor_half = (cq.Workplane("XY").box(20, 60, 80, centered=(False, True, True))
              .rotate((0, 0, 0), (0, 1, 0), tilt)
              .translate((WIN_X_FLOOR_BOT + (WIN_X_FLOOR_TOP - WIN_X_FLOOR_BOT) * 0.5, 0,
                          (WIN_Z_TOP + WIN_Z_LOW) / 2)))
body = body.cut(win.intersect(floor_half))


def win_floor_x(z):
    """X position of the main (tilted) window floor at height z."""
    zm = (WIN_Z_TOP + WIN_Z_LOW) / 2
    return (WIN_X_FLOOR_BOT + WIN_X_FLOOR_TOP) / 2 + (z - zm) * math.tan(math.radians(tilt))


# second floor facet left of a slanted crease: the recess gets deeper towards its -Y wall
c_top, c_bot = WIN_CREASE
p1 = cq.Vector(win_floor_x(c_top[1]), c_top[0], c_top[1])
p2 = cq.Vector(win_floor_x(c_bot[1]), c_bot[0], c_bot[1])
zc = (c_top[1] + c_bot[1]) / 2
p3 = cq.Vector(win_floor_x(zc) - WIN_FACET_DROP, -WIN_HALF_W, zc)
n2 = (p2 - p1).cross(p3 - p1).normalized()
if n2.x < 0:
    n2 = n2 * -1.0
facet_half = (cq.Workplane(cq.Plane(origin=p1.toTuple(), xDir=(p2 - p1).normalized().toTuple(), normal=n2.toTuple()))
              .rect(200, 200).extrude(30))
body = body.cut(win.intersect(facet_half))

# slotted plug on the +X side of the top band
r_band = R_BODY - BAND_INSET
plug = (cq.Workplane("YZ").workplane(offset=r_band - 1.5).center(0, PLUG_Z)
        .circle(PLUG_R).extrude(1.5 + PLUG_PROUD)
        .faces(">X").chamfer(0.4))
for dz in (-0.6, 0.6):
    plug = plug.cut(cq.Workplane("XY").box(1.0, 4.6, 0.3).translate((r_band + PLUG_PROUD, 0, PLUG_Z + dz)))
body = body.union(plug)
# vertical seams of the strip around the plug
for sy in (-1, 1):
    body = body.cut(cq.Workplane("XY").box(6, GROOVE_W, H_BODY - Z_BAND, centered=(False, True, False))
                    .translate((r_band - 3.0, sy * (PLUG_R + 0.45), Z_BAND))
                    .cut(cq.Workplane("XY").circle(r_band - GROOVE_D).extrude(H_BODY + 5)))

# further parting seams in the top band: a vertical one at the front-right and a slanted one at the back-right
band_skin = (d_prism(4.0, Z_BAND, H_BODY)
             .cut(d_prism(-BAND_INSET - GROOVE_D, Z_BAND - 1.0, H_BODY + 2.0)))


def band_seam(p0, p1):
    """Thin slab through two points on the band surface (radial orientation), limited to the band skin."""
    v0, v1 = cq.Vector(*p0), cq.Vector(*p1)
    mid = (v0 + v1) * 0.5
    along = (v1 - v0)
    radial = cq.Vector(mid.x, mid.y, 0).normalized()
    normal = along.cross(radial).normalized()
    L = along.Length + 6.0
    slab = (cq.Workplane(cq.Plane(origin=mid.toTuple(), xDir=along.normalized().toTuple(), normal=normal.toTuple()))
            .rect(L, 12.0).extrude(GROOVE_W / 2, both=True))
    return slab.intersect(band_skin)


a_v = math.radians(-44.4)
body = body.cut(band_seam((r_band * math.cos(a_v), r_band * math.sin(a_v), Z_BAND - 1),
                          (r_band * math.cos(a_v), r_band * math.sin(a_v), H_BODY + 1)))
a0, a1 = math.radians(8.4), math.radians(20.3)
body = body.cut(band_seam((r_band * math.cos(a0), r_band * math.sin(a0), H_BODY),
                          (r_band * math.cos(a1), r_band * math.sin(a1), Z_BAND)))

# service flap on the rear face (-X), wrapping over the sloped top
FLAP_Y, FLAP_W, FLAP_Z0 = 13.65, 17.9, 46.4
flap_region = (cq.Workplane("XY").box(X_BACK + 2.5 - (X_BACK - 3.0), FLAP_W, 40.0, centered=(False, True, False))
               .translate((X_BACK - 3.0, FLAP_Y, FLAP_Z0)))
flap = housing(0.7).intersect(flap_region)
body = body.union(flap)
# small latch on the rear face
body = body.union(cq.Workplane("XY").box(1.6, 4.0, 1.5).translate((X_BACK, 1.1, 26.9)))


# ------------------------------------------------------------------ screw bosses
def boss_on_face(center, normal):
    """Square screw boss with a counterbored socket screw; center = point on outer boss face."""
    nx, ny = normal
    depth = 5.0
    d = cq.Vector(nx, ny, 0)
    if nx != 0:
        b = cq.Workplane("XY").box(depth, BOSS_W, BOSS_H).edges("|X").fillet(1.0)
    else:
        b = cq.Workplane("XY").box(BOSS_W, depth, BOSS_H).edges("|Y").fillet(1.0)
    c = cq.Vector(*center)
    b = b.translate(c - d * (depth / 2.0))
    b = b.faces(">X" if nx > 0 else "<X" if nx < 0 else ">Y" if ny > 0 else "<Y").edges().chamfer(0.3)
    cb = cq.Solid.makeCylinder(2.4, 1.4, c - d * 1.4, d)
    head = cq.Solid.makeCylinder(1.9, 1.0, c - d * 1.4, d)
    sock = cq.Solid.makeCylinder(0.9, 0.8, c - d * 0.7, d)
    b = b.cut(cq.Workplane().add(cb)).union(cq.Workplane().add(head)).cut(cq.Workplane().add(sock))
    return b


for bx in BOSS_X_SIDE:
    for sy in (-1, 1):
        body = body.union(boss_on_face((bx, sy * (R_BODY + BOSS_PROUD), BOSS_Z), (0, sy)))
for by in BOSS_Y_BACK:
    body = body.union(boss_on_face((X_BACK - BOSS_PROUD_BACK, by, BOSS_Z), (-1, 0)))

# small screws on the housing top at the rear corners, sitting in corner notches
for sy in (-1, 1):
    nx0, nx1 = CORNER_NOTCH_X
    ny0, ny1 = CORNER_NOTCH_Y
    notch = (cq.Workplane("XY").box(nx1 - (X_BACK - 2.0), ny1 - ny0, 20.0, centered=False)
             .edges("|Z and >X").fillet(1.0)
             .translate((X_BACK - 2.0, ny0, CORNER_NOTCH_Z)))
    if sy > 0:
        notch = notch.mirror("XZ")
    body = body.cut(notch)
    p = (CORNER_SCREW[0], sy * CORNER_SCREW[1])
    body = body.union(cq.Workplane("XY").workplane(offset=CORNER_NOTCH_Z - 0.5).center(*p)
                      .circle(1.65).extrude(1.1).faces(">Z").chamfer(0.3))
    body = body.cut(cq.Workplane("XY").workplane(offset=CORNER_NOTCH_Z + 0.1).center(*p)
                    .polygon(6, 1.4).extrude(1))

# ------------------------------------------------------------------ raised SICK logo on both sides
for sy in (-1, 1):
    # letters read upward on the front (-Y) and downward on the back (+Y)
    plane = cq.Plane(origin=(LOGO_X, sy * (R_BODY - 1.2), LOGO_Z),
                     xDir=(0, 0, 1) if sy < 0 else (0, 0, -1),
                     normal=(0, sy, 0))
    txt = (cq.Workplane(plane)
           .text("SICK", LOGO_H, 2.0, kind="bold", halign="center", valign="center"))
    logo = txt.intersect(cq.Workplane("XY").circle(R_BODY + 0.3).extrude(H_BODY))
    body = body.union(logo)

# ------------------------------------------------------------------ optics head (revolved)
head = (cq.Workplane("XZ")
        .moveTo(0, H_BODY - 0.5)
        .lineTo(R_RING, H_BODY - 0.5)
        .lineTo(R_RING, Z_RING_WALL - 0.6)
        .threePointArc((R_RING - 0.18, Z_RING_WALL + 0.05), (R_RING - 0.7, Z_RING_WALL + 0.3))
        .lineTo(R_RING_IN, Z_RING_TOP)
        .lineTo(R_CONE_BOT, Z_CONE_BOT)
        .lineTo(R_CONE_TOP, Z_CONE_TOP)
        .lineTo(R_CONE_LIP, Z_CAP_BOT)
        .lineTo(R_CAP_BOT, Z_CAP_BOT)
        .lineTo(R_CAP_TOP, Z_CAP_EDGE)
        .lineTo(R_STEP, Z_CAP_EDGE)
        .lineTo(R_PLATEAU, Z_PLATEAU)
        .lineTo(0, Z_PLATEAU)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), HEAD_SEAM_ANGLE))


def circle_edges(wp, r, z, tol=0.05):
    out = []
    for e in wp.edges().vals():
        if e.geomType() == "CIRCLE" and abs(e.radius() - r) < tol and abs(e.Center().z - z) < tol:
            out.append(e)
    return wp.newObject(out)


head = circle_edges(head, R_CAP_TOP, Z_CAP_EDGE).fillet(CAP_EDGE_FILLET)
head = circle_edges(head, R_STEP, Z_CAP_EDGE).fillet(STEP_FILLET)
head = circle_edges(head, R_PLATEAU, Z_PLATEAU).fillet(STEP_FILLET)

# centre hole on the cap
head = head.cut(cq.Workplane("XY").workplane(offset=Z_PLATEAU - 1.0).circle(0.9).extrude(3))
# shallow groove on the ring top
rg = 26.4
zg = Z_RING_WALL + (R_RING - rg) / (R_RING - R_RING_IN) * (Z_RING_TOP - Z_RING_WALL)
head = head.cut(cq.Workplane("XY").workplane(offset=zg - 0.3).circle(rg + 0.2).circle(rg - 0.2).extrude(2))

# screws on the ring
for ang in (-60.0, 60.0, 180.0):
    a = math.radians(ang)
    rs = 29.1
    zs = Z_RING_WALL + (R_RING - rs) / (R_RING - R_RING_IN) * (Z_RING_TOP - Z_RING_WALL)
    c = (rs * math.cos(a), rs * math.sin(a))
    head = head.cut(cq.Workplane("XY").workplane(offset=zs - 0.3).center(*c).circle(1.9).extrude(3))
    head = head.union(cq.Workplane("XY").workplane(offset=zs - 1.0).center(*c).circle(1.5).extrude(1.2))
    head = head.cut(cq.Workplane("XY").workplane(offset=zs - 0.2).center(*c).polygon(6, 1.3).extrude(1))

body = body.union(head)

# ------------------------------------------------------------------ connectors (M12)
for cy in CONN_Y:
    c = (cq.Workplane("XY").workplane(offset=0.5).center(CONN_X, cy)
         .circle(CONN_BASE_R).extrude(-(CONN_BASE_H + 0.5))
         .faces("<Z").chamfer(0.35))
    c = c.union(cq.Workplane("XY").workplane(offset=-CONN_BASE_H + 0.1).center(CONN_X, cy)
                .polygon(6, CONN_NUT_AF / math.cos(math.pi / 6)).extrude(-(CONN_NECK_H + 0.1))
                .edges("<Z or >Z").chamfer(0.3))
    c = c.union(cq.Workplane("XY").workplane(offset=-CONN_BASE_H - CONN_NECK_H + 0.1).center(CONN_X, cy)
                .circle(CONN_TIP_R).extrude(-(CONN_LEN - CONN_BASE_H - CONN_NECK_H + 0.1))
                .faces("<Z").chamfer(0.3))
    c = c.cut(cq.Workplane("XY").workplane(offset=-CONN_LEN).center(CONN_X, cy)
              .circle(CONN_TIP_R - 1.6).extrude(2.5))
    body = body.union(c)

# pressure compensation elements in the bottom of the rear corners
for sy in (-1, 1):
    p = (-34.3, sy * 33.0)
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(*p).circle(2.3).circle(1.9).extrude(1.5))
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(*p).circle(0.7).extrude(1.6))

# small screws in the bottom cover
for p in ((16.0, -28.0), (16.0, 28.0)):
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(*p).circle(2.3).extrude(1.8))
    body = body.union(cq.Workplane("XY").workplane(offset=0.8).center(*p).circle(1.9).extrude(-0.5))
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(*p).polygon(6, 1.6).extrude(1.5))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
